import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Electrical junction box ("AERO GUARD") with separate cover plate.
# Box: open-top shell with conduit boss on the -Y end, cover lies beside it (+X).
# ---------------------------------------------------------------------------

# ---- box main dimensions ----
W = 100.0          # box width  (X)
L = 164.0          # box length (Y)
H = 52.6           # box height (Z)
WALL = 4.3         # side wall thickness
FLOOR = 6.0        # floor thickness
R_OUT = 3.5        # outer vertical corner radius
R_EDGE_TOP = 0.5   # outer top edge round
R_EDGE_BOT = 0.5   # outer bottom edge round
R_IN = 4.5         # inner cavity corner radius
CH_IN = 0.7        # chamfer on inner top edge

# ---- corner screw bosses (diagonal corners) ----
SCREW_TR = (W / 2 - 9.3, L / 2 - 11.0)    # (+X,+Y) corner
SCREW_BL = (-W / 2 + 9.0, -L / 2 + 8.6)   # (-X,-Y) corner
R_SBOSS = 8.2      # boss radius around screw
R_SBOSS_FIL = 3.8  # blend radius boss -> wall
D_SCREW = 4.5      # tapped hole dia
SCREW_DEPTH = 14.0
SCREW_CH = 1.75

# ---- conduit hub on the -Y end ----
HUB_X = 2.7        # hub axis offset in X
HUB_Z = 27.0       # hub axis height
HUB_R_END = 17.0   # hub radius at its end face
HUB_R_FACE = 24.0  # flare radius where it meets the wall (tangent)
HUB_LEN = 13.6     # hub protrusion
HUB_BORE = 29.4    # bore diameter
HUB_BORE_FIL = 1.5  # round on the bore mouth

# ---- small holes in the -Y end wall ----
SMALL_HOLES = [(26.4, 37.6), (26.4, 16.4)]   # (x, z)
D_SMALL = 3.6
BIG_HOLE = (35.7, 12.5)
D_BIG = 9.0

# ---- slot in the +X side wall ----
SLOT_Y = 50.0
SLOT_Z = 8.8
SLOT_LEN = 15.0
SLOT_H = 5.0
SLOT_R = 1.3

# ---- cover plate ----
GAP = 10.0         # gap between box and cover
T_LID = 7.0        # cover thickness
R_LID_TOP = 3.0    # top edge round
R_LID_BOT = 0.8    # bottom edge round
LID_HOLES = [(W / 2 - 9.3, L / 2 - 10.7), (-W / 2 + 9.3, -L / 2 + 8.8)]
D_LID_HOLE = 6.6
D_LID_CSK = 11.5
TEXT = "AERO GUARD"
TEXT_SIZE = 17.3
TEXT_DEPTH = 1.0   # engraved lettering depth

LID_X = W + GAP    # cover centre X


# =========================== box ===========================
box = (
    cq.Workplane("XY")
    .box(W, L, H, centered=(True, True, False))
    .edges("|Z").fillet(R_OUT)
    .faces(">Z").edges().fillet(R_EDGE_TOP)
    .faces("<Z").edges().fillet(R_EDGE_BOT)
)

# cavity tool: rounded rectangle minus the two corner screw bosses, blended
cav_w = W - 2 * WALL
cav_l = L - 2 * WALL
cav_h = H - FLOOR
cavity = (
    cq.Workplane("XY", origin=(0, 0, FLOOR))
    .rect(cav_w, cav_l)
    .extrude(cav_h + 5)
    .edges("|Z").fillet(R_IN)
)
for (sx, sy) in (SCREW_TR, SCREW_BL):
    cyl = cq.Workplane("XY", origin=(sx, sy, FLOOR - 1)).circle(R_SBOSS).extrude(cav_h + 10)
    cavity = cavity.cut(cyl)


def _near_boss(e):
    c = e.Center()
    for (sx, sy) in (SCREW_TR, SCREW_BL):
        if math.hypot(c.x - sx, c.y - sy) < R_SBOSS + 1.0:
            return True
    return False


class _BossJunction(cq.Selector):
    def filter(self, objs):
        out = []
        for o in objs:
            if o.geomType() != "LINE":
                continue
            d = o.endPoint() - o.startPoint()
            if abs(d.x) > 1e-6 or abs(d.y) > 1e-6:
                continue
            if _near_boss(o):
                out.append(o)
        return out


cavity = cavity.edges(_BossJunction()).fillet(R_SBOSS_FIL)
box = box.cut(cavity)


# chamfer the inner top edge of the rim
class _InnerRim(cq.Selector):
    def filter(self, objs):
        out = []
        for o in objs:
            c = o.Center()
            if abs(c.z - H) > 1e-3:
                continue
            if abs(c.x) < W / 2 - WALL + 0.05 + 1.0 and abs(c.y) < L / 2 - WALL + 0.05 + 1.0:
                # keep only edges lying on the cavity outline (not the outer fillet boundary)
                if abs(c.x) < W / 2 - R_EDGE_TOP - 0.5 and abs(c.y) < L / 2 - R_EDGE_TOP - 0.5:
                    out.append(o)
        return out


try:
    box = box.edges(_InnerRim()).chamfer(CH_IN)
except Exception:
    pass

# screw holes in the corner bosses
for (sx, sy) in (SCREW_TR, SCREW_BL):
    hole = (
        cq.Workplane("XY", origin=(sx, sy, H - SCREW_DEPTH))
        .circle(D_SCREW / 2).extrude(SCREW_DEPTH + 1)
    )
    csk = cq.Solid.makeCone(D_SCREW / 2, D_SCREW / 2 + SCREW_CH + 1.0, SCREW_CH + 1.0,
                            pnt=cq.Vector(sx, sy, H - SCREW_CH), dir=cq.Vector(0, 0, 1))
    box = box.cut(hole).cut(cq.Workplane().add(csk))

# ---- conduit hub: revolved profile with an elliptical flare, axis along -Y ----
# (built about +Z first, then turned so that +Z -> -Y)
_d = HUB_R_FACE - HUB_R_END
_flare = cq.Edge.makeEllipse(_d, HUB_LEN, pnt=cq.Vector(HUB_R_FACE, 0, HUB_LEN), dir=cq.Vector(0, 1, 0),
                             xdir=cq.Vector(1, 0, 0), angle1=90, angle2=180, sense=1)
_p0 = cq.Vector(0, 0, -2.0)
_p1 = cq.Vector(HUB_R_FACE, 0, -2.0)
_p2 = cq.Vector(HUB_R_FACE, 0, 0)
_p3 = cq.Vector(HUB_R_END, 0, HUB_LEN)
_p4 = cq.Vector(0, 0, HUB_LEN)
_wire = cq.Wire.assembleEdges([
    cq.Edge.makeLine(_p0, _p1),
    cq.Edge.makeLine(_p1, _p2),
    _flare,
    cq.Edge.makeLine(_p3, _p4),
    cq.Edge.makeLine(_p4, _p0),
])
hub = cq.Solid.revolve(cq.Face.makeFromWires(_wire), 360, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
hub = hub.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90).translate(cq.Vector(HUB_X, -L / 2, HUB_Z))
box = box.union(cq.Workplane().add(hub))

# bore through hub and wall, mouth rounded
bore = cq.Solid.makeCylinder(HUB_BORE / 2, HUB_LEN + WALL + 6,
                             pnt=cq.Vector(HUB_X, -L / 2 - HUB_LEN - 1, HUB_Z), dir=cq.Vector(0, 1, 0))
box = box.cut(cq.Workplane().add(bore))


class _BoreMouth(cq.Selector):
    def filter(self, objs):
        out = []
        for o in objs:
            if o.geomType() != "CIRCLE":
                continue
            c = o.Center()
            if (abs(c.x - HUB_X) < 1e-2 and abs(c.z - HUB_Z) < 1e-2 and abs(c.y + L / 2 + HUB_LEN) < 1e-2
                    and abs(o.radius() - HUB_BORE / 2) < 1e-2):
                out.append(o)
        return out


try:
    box = box.edges(_BoreMouth()).fillet(HUB_BORE_FIL)
except Exception:
    pass

# small holes in the -Y end wall
for (hx, hz) in SMALL_HOLES:
    h = cq.Solid.makeCylinder(D_SMALL / 2, WALL + 4, pnt=cq.Vector(hx, -L / 2 - 2, hz), dir=cq.Vector(0, 1, 0))
    box = box.cut(cq.Workplane().add(h))
h = cq.Solid.makeCylinder(D_BIG / 2, WALL + 4, pnt=cq.Vector(BIG_HOLE[0], -L / 2 - 2, BIG_HOLE[1]),
                          dir=cq.Vector(0, 1, 0))
box = box.cut(cq.Workplane().add(h))

# rounded-rectangle slot through the +X side wall
slot = (
    cq.Workplane("XY")
    .box(WALL + 4, SLOT_LEN, SLOT_H)
    .edges("|X").fillet(SLOT_R)
    .translate((W / 2 - WALL / 2, SLOT_Y, SLOT_Z))
)
box = box.cut(slot)

# =========================== cover ===========================
lid = (
    cq.Workplane("XY")
    .box(W, L, T_LID, centered=(True, True, False))
    .edges("|Z").fillet(R_OUT)
    .faces(">Z").edges().fillet(R_LID_TOP)
    .faces("<Z").edges().fillet(R_LID_BOT)
)
lid = lid.faces(">Z").workplane(origin=(0, 0, T_LID)).pushPoints(LID_HOLES).cskHole(D_LID_HOLE, D_LID_CSK, 90)

# engraved lettering, reading along -Y with letter tops toward +X
try:
    txt = cq.Workplane(cq.Plane(origin=(0, 0, T_LID - TEXT_DEPTH), xDir=(0, -1, 0), normal=(0, 0, 1))).text(
        TEXT, TEXT_SIZE, TEXT_DEPTH + 1.0, kind="bold", font="DejaVu Sans", halign="center", valign="center"
    )
    lid = lid.cut(txt)
except Exception:
    pass

lid = lid.translate((LID_X, 0, 0))

result = box.union(lid)
